import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BX = 27.4          # servo case width (X), without side plate
BY = 46.5          # case length (Y)
BZ = 31.2          # case height (Z)
BODY_CH = 1.4      # vertical edge chamfer of the case

PT = 4.0           # side plate thickness (+X side)
P_VCH = 2.8        # side plate vertical outer edge chamfer
P_HCH = 1.3        # side plate horizontal outer edge chamfer

HH = 3.74          # horn height above case top
IH = 3.98          # idler height below case bottom
HX, HY = 13.7, 10.4  # horn / idler axis position
HR = 10.9          # horn radius
H_HOLE_R = 8.1     # horn bolt circle radius
H_HOLE_D = 2.2

TAB_H = 1.9        # corner tab height above case top
TAB_X0 = 22.0

HOLE_D = 2.3       # case through holes
SCREW_D = 3.8      # case screw head dia

SPLIT_TOP = 5.6    # split lines from the top / bottom
SPLIT_BOT = 6.9

Z_TOP = BZ / 2.0
Z_BOT = -BZ / 2.0
PX1 = BX + PT      # outer face of side plate
PZ0 = Z_BOT - IH
PZ1 = Z_TOP + HH
PZC = 0.5 * (PZ0 + PZ1)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0)
            .translate(((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2)))


def cyl_z(x, y, r, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center(x, y).circle(r).extrude(z1 - z0))


# ---------------- main case ----------------
EDGE_CH = 0.3      # small bevel around the case top and bottom
body = (box(0, BX, -BY / 2, BY / 2, Z_BOT, Z_TOP).edges("|Z").chamfer(BODY_CH)
        .faces(">Z or <Z").edges().chamfer(EDGE_CH))

# ---------------- side plate (+X) ----------------
plate_pts = [
    (BX, -BY / 2), (PX1 - P_VCH, -BY / 2), (PX1, -BY / 2 + P_VCH),
    (PX1, BY / 2 - P_VCH), (PX1 - P_VCH, BY / 2), (BX, BY / 2),
]
plate = (cq.Workplane("XY").workplane(offset=PZ0)
         .polyline(plate_pts).close().extrude(PZ1 - PZ0))
plate = plate.edges(
    cq.selectors.BoxSelector((BX + 0.3, -BY, PZ1 - 0.01), (PX1 + 1, BY, PZ1 + 0.01))
).chamfer(P_HCH)
plate = plate.edges(
    cq.selectors.BoxSelector((BX + 0.3, -BY, PZ0 - 0.01), (PX1 + 1, BY, PZ0 + 0.01))
).chamfer(P_HCH)


# ---------------- raised rim next to the plate (top and bottom) -------
def _tangent_arc_mid(x_in, y_t, px, py):
    """mid point of an arc that is tangent to the line x = x_in at (x_in, y_t)
    and passes through (px, py); the arc centre lies on y = y_t."""
    dx = x_in - px
    dy = py - y_t
    r = (dx * dx + dy * dy) / (2.0 * dx)
    cx = x_in - r
    a1 = math.atan2(py - y_t, px - cx)
    am = 0.5 * a1
    return (cx + r * math.cos(am), y_t + r * math.sin(am))


TAB_YB = 17.98     # inner edge of the back corner tabs
TAB_YF = -17.6     # inner edge of the front corner tabs
TAB_RC = 1.6       # rounding of the tab corner next to the plate
_c45 = math.cos(math.radians(45))


def rim_sketch(wp, x_in, y_b, y_f):
    """outline of the raised rim; x_in = inner edge along the plate,
    y_b / y_f = where the back / front blend arcs meet that edge."""
    return (wp.moveTo(22.4, TAB_YB)
            .threePointArc(_tangent_arc_mid(x_in, y_b, 22.4, TAB_YB), (x_in, y_b))
            .lineTo(x_in, y_f)
            .threePointArc(_tangent_arc_mid(x_in, y_f, 22.2, TAB_YF), (22.2, TAB_YF))
            .lineTo(BX + 1.0, TAB_YF)
            .lineTo(BX + 1.0, TAB_YB)
            .close())


def rim_fillers(z0, h):
    """rim material wrapping the rounded inner corners of the corner tabs."""
    r = TAB_RC
    out = None
    for (yc, ys) in ((TAB_YF - r, TAB_YF - r), (TAB_YB + r, TAB_YB)):
        blk = box(BX - r, BX + 1.0, ys, ys + r, min(z0, z0 + h), max(z0, z0 + h))
        blk = blk.cut(cyl_z(BX - r, yc, r, min(z0, z0 + h) - 1, max(z0, z0 + h) + 1))
        out = blk if out is None else out.union(blk)
    return out


RIM_T_X = 27.0     # inner edge of the top rim
RIM_B_X = 26.0     # inner edge of the (wider) bottom rim

RIM_FIL = 0.6


def fillet_inner_top(wp, face_sel):
    """round the inner (horn side) top edges of a rim solid only."""
    solid = wp.val()
    keep = []
    for e in wp.faces(face_sel).edges().vals():
        c = e.Center()
        if c.x > BX + 0.5:
            continue
        if e.geomType() == "LINE" and (abs(c.y - TAB_YF) < 1e-3 or abs(c.y - TAB_YB) < 1e-3):
            continue
        keep.append(e)
    return cq.Workplane("XY").newObject([solid.fillet(RIM_FIL, keep)])


rim_top = fillet_inner_top(
    rim_sketch(cq.Workplane("XY").workplane(offset=Z_TOP), RIM_T_X, 8.5, -10.1).extrude(HH), ">Z")
rim_bot = fillet_inner_top(
    rim_sketch(cq.Workplane("XY").workplane(offset=Z_BOT), RIM_B_X, 8.5, -12.6).extrude(-IH), "<Z")
rim_top = rim_top.union(rim_fillers(Z_TOP, HH))
rim_bot = rim_bot.union(rim_fillers(Z_BOT, -IH))


def rounded_rect(wp, x0, x1, y0, y1, r):
    """rectangle with individual corner radii r = (r00, r10, r11, r01)
    for the corners (x0,y0), (x1,y0), (x1,y1), (x0,y1); 0 = sharp."""
    r00, r10, r11, r01 = r
    w = wp.moveTo(x0 + r00, y0).lineTo(x1 - r10, y0)
    if r10 > 0:
        w = w.threePointArc((x1 - r10 + r10 * _c45, y0 + r10 - r10 * _c45), (x1, y0 + r10))
    w = w.lineTo(x1, y1 - r11)
    if r11 > 0:
        w = w.threePointArc((x1 - r11 + r11 * _c45, y1 - r11 + r11 * _c45), (x1 - r11, y1))
    w = w.lineTo(x0 + r01, y1)
    if r01 > 0:
        w = w.threePointArc((x0 + r01 - r01 * _c45, y1 - r01 + r01 * _c45), (x0, y1 - r01))
    w = w.lineTo(x0, y0 + r00)
    if r00 > 0:
        w = w.threePointArc((x0 + r00 - r00 * _c45, y0 + r00 - r00 * _c45), (x0 + r00, y0))
    return w.close()


TAB_X0_F = 22.0    # front tabs


def corner_tabs(z0, h):
    wp = cq.Workplane("XY").workplane(offset=z0)
    back = rounded_rect(wp, TAB_X0, BX, TAB_YB, BY / 2, (1.5, TAB_RC, 0, 1.5)).extrude(h)
    wp = cq.Workplane("XY").workplane(offset=z0)
    front = rounded_rect(wp, TAB_X0_F, BX, -BY / 2, TAB_YF, (1.0, 0, TAB_RC, 0.4)).extrude(h)
    return back.union(front)


tabs = corner_tabs(Z_TOP, TAB_H).union(corner_tabs(Z_BOT, -TAB_H))

# ---------------- horn and idler ----------------
horn = cyl_z(HX, HY, HR, Z_TOP, PZ1).faces(">Z").edges().chamfer(0.35)
idler = cyl_z(HX, HY, HR, PZ0, Z_BOT).faces("<Z").edges().chamfer(0.35)

part = body.union(plate).union(rim_top).union(rim_bot).union(tabs)
part = part.union(horn).union(idler)

# horn / idler bolt holes and centre recess
for zs, sgn in ((PZ1, -1), (PZ0, 1)):
    for k in range(4):
        a = math.radians(45 + 90 * k)
        hx = HX + H_HOLE_R * math.cos(a)
        hy = HY + H_HOLE_R * math.sin(a)
        za, zb = zs - sgn * 1.0, zs + sgn * 3.0      # 3 mm deep bolt holes
        part = part.cut(cyl_z(hx, hy, H_HOLE_D / 2, min(za, zb), max(za, zb)))
    # centre recess
    if sgn < 0:
        part = part.cut(cyl_z(HX, HY, 4.2, zs - 0.8, zs + 1))
    else:
        part = part.cut(cyl_z(HX, HY, 5.5, zs - 1, zs + 1.4))


def pan_screw(x, y, z_base, d, h_cyl, h_dome, up=True, rot=0.0):
    """pan head screw with a cross recess, sitting on z_base."""
    r = d / 2.0
    s = 1 if up else -1
    head = cyl_z(x, y, r, min(z_base, z_base + s * h_cyl), max(z_base, z_base + s * h_cyl))
    R = (r * r + h_dome * h_dome) / (2 * h_dome)
    zc = z_base + s * (h_cyl + h_dome - R)
    sph = cq.Workplane("XY").sphere(R).translate((x, y, zc))
    zt = z_base + s * h_cyl
    lim = box(x - r, x + r, y - r, y + r,
              min(zt, zt + s * h_dome), max(zt, zt + s * h_dome))
    head = head.union(sph.intersect(lim))
    ztop = z_base + s * (h_cyl + h_dome)
    w = 0.12 * d
    ln = 0.62 * d
    dep = 0.5 * h_dome + 0.2
    for (lx, ly) in ((ln, w), (w, ln)):
        c = box(-lx / 2, lx / 2, -ly / 2, ly / 2,
                min(ztop, ztop - s * dep) - 0.01, max(ztop, ztop - s * dep) + 0.01)
        c = c.rotate((0, 0, 0), (0, 0, 1), rot).translate((x, y, 0))
        head = head.cut(c)
    return head


# centre screws of horn and idler
part = part.union(pan_screw(HX, HY, PZ1 - 0.8, 7.5, 0.25, 1.61, up=True, rot=45))
part = part.union(pan_screw(HX, HY, PZ0 + 1.4, 7.6, 0.35, 0.95, up=False, rot=45))

# ---------------- case through holes at the corners ----------------
corner_holes = [(2.75, 20.65), (2.75, -20.55), (24.7, 20.7), (24.7, -20.45)]
for (cx, cy) in corner_holes:
    part = part.cut(cyl_z(cx, cy, HOLE_D / 2, PZ0 - 1, PZ1 + 1))
    # small countersink at the top
    ztop = Z_TOP + (TAB_H if cx > 20 else 0.0)
    cs = (cq.Workplane("XY").workplane(offset=ztop - 0.35).center(cx, cy)
          .circle(HOLE_D / 2).workplane(offset=0.36).circle(HOLE_D / 2 + 0.36).loft())
    part = part.cut(cs)

# ---------------- screw pockets with screws ----------------
POCK_D = 2.0
pockets = [
    # (x, y, open direction)
    (2.3, 16.5, "-x"),
    (2.2, -16.3, "-x"),
    (20.0, -21.05, "-y"),
]
for (sx, sy, od) in pockets:
    r = SCREW_D / 2 + 0.2
    z0, z1 = Z_TOP - POCK_D, Z_TOP + 0.01
    pk = cyl_z(sx, sy, r, z0, z1)
    if od == "-x":
        pk = pk.union(box(-1, sx, sy - r, sy + r, z0, z1))
    else:
        pk = pk.union(box(sx - r, sx + r, -BY / 2 - 1, sy, z0, z1))
    part = part.cut(pk)
    part = part.union(pan_screw(sx, sy, Z_TOP - POCK_D, SCREW_D, 0.4, 1.45, up=True))

# ---------------- label recess on top ----------------
label = (cq.Workplane("XY").workplane(offset=Z_TOP - 0.3)
         .center((4.68 + 22.87) / 2, (-6.74 - 14.7) / 2)
         .rect(22.87 - 4.68, 14.7 - 6.74).extrude(1.0)
         .edges("|Z").fillet(0.8))
part = part.cut(label)

# ---------------- side plate hole pattern ----------------
small = [(14.4, 12.3, 2.8), (5.6, 10.9, 2.2), (17.9, 7.8, 2.8), (10.3, 8.2, 2.8),
         (2.5, 7.8, 2.8), (18.4, 0.0, 2.8), (2.0, 0.0, 2.8)]
pts = set()
for (py, pz, d) in small:
    for sy in (1, -1):
        for sz in (1, -1):
            pts.add((sy * py, sz * pz, d))
for (py, pz, d) in sorted(pts):
    h = (cq.Workplane("YZ").workplane(offset=PX1 - 6.0)
         .center(py, PZC + pz).circle(d / 2).extrude(7.0))
    part = part.cut(h)
BIG_Y = 10.2
BIG_D = 10.9
BIG_DEPTH = 3.2
for py in (BIG_Y, -BIG_Y):
    h = (cq.Workplane("YZ").workplane(offset=PX1 - BIG_DEPTH)
         .center(py, PZC).circle(BIG_D / 2).extrude(BIG_DEPTH + 1.0))
    part = part.cut(h)
    # internal notches in the wall of the big holes (below the surface)
    for adeg in (45, 90, 135, 225, 270, 315):
        a = math.radians(adeg)
        nb = box(PX1 - BIG_DEPTH, PX1 - 1.0, -0.8, 0.8, BIG_D / 2 - 0.5, BIG_D / 2 + 0.8)
        nb = nb.rotate((0, 0, 0), (1, 0, 0), math.degrees(a)).translate((0, py, PZC))
        part = part.cut(nb)
# key block inside the -Y big hole (lower +Y quadrant)
kb = box(PX1 - BIG_DEPTH - 0.1, PX1 - 1.3, -BIG_Y + 1.0, -BIG_Y + BIG_D / 2 + 0.2,
         PZC - BIG_D / 2 - 0.2, PZC - 0.55 * BIG_D / 2)
kb = kb.intersect(cq.Workplane("YZ").workplane(offset=PX1 - BIG_DEPTH - 0.2)
                  .center(-BIG_Y, PZC).circle(BIG_D / 2 + 0.01).extrude(BIG_DEPTH))
part = part.union(kb)

# ---------------- split lines on the case ----------------
for zl in (Z_TOP - SPLIT_TOP, Z_BOT + SPLIT_BOT):
    ring = box(-1, BX - 0.5, -BY / 2 - 1, BY / 2 + 1, zl - 0.06, zl + 0.06).cut(
        box(0.12, BX, -BY / 2 + 0.12, BY / 2 - 0.12, zl - 1, zl + 1))
    part = part.cut(ring)

# ---------------- connector pocket on -X face ----------------
CY0, CY1 = -9.4, 5.45
CON_H = 12.3
part = part.cut(box(-1, 3.0, CY0, CY1, Z_BOT - 1, Z_BOT + CON_H))
conn = box(0.6, 3.0, CY0 + 0.7, CY1 - 0.7, Z_BOT + CON_H - 5.4, Z_BOT + CON_H - 0.6)
for k in range(6):
    yy = CY0 + 2.0 + k * 2.1
    conn = conn.cut(box(0.4, 2.2, yy - 0.4, yy + 0.4, Z_BOT + CON_H - 5.6, Z_BOT + CON_H - 1.6))
part = part.union(conn)
# centre divider in the lower, open part of the connector pocket
part = part.union(box(1.2, 3.0, -2.4, -1.6, Z_BOT, Z_BOT + CON_H - 5.4))

# small notch in the back face at the bottom edge
part = part.cut(box(10.7, 19.5, BY / 2 - 0.8, BY / 2 + 1, Z_BOT - 1, Z_BOT + 1.8))

# windows under the lip of the top rim
for (wy0, wy1) in ((-8.5, -4.0), (-2.8, 1.7), (2.9, 6.0)):
    part = part.cut(box(26.2, 28.2, wy0, wy1, Z_TOP + 0.25, Z_TOP + HH - 1.0))

# groove along the bottom rim
groove = (cq.Workplane("XY").workplane(offset=PZ0 - 1)
          .center(26.65, -5.1).slot2D(15.8, 0.9, 90).extrude(1.0 + 1.0))
part = part.cut(groove)

# alignment tick behind the horn
part = part.cut(box(HX - 0.35, HX + 0.35, BY / 2 - 2.0, BY / 2 + 1, Z_TOP - 0.3, Z_TOP + 1))

result = part
